import cadquery as cq

# ---------------------------------------------------------------------------
# Flat base plate (robot-chassis style) standing in the XZ plane, thickness
# along Y.  Rounded-rectangle outline, two vertical hand-hold slots, one long
# horizontal slot near the top edge and a symmetric field of mounting holes
# (the top edge has the long slot where the bottom edge has four holes).
# ---------------------------------------------------------------------------

# ---------------- driving dimensions (mm) ----------------
W = 200.0          # plate width  (X)
H = 306.5          # plate height (Z)
T = 4.0            # plate thickness (Y)
R_CORNER = 31.5    # outline corner radius

# side hand-hold slots (vertical, through)
HANDLE_X = 76.75   # slot centre offset from the plate centre
HANDLE_W = 23.0    # slot width
HANDLE_L = 84.0    # slot overall length

# long slot near the top edge (horizontal, through)
TSLOT_Z = 137.8    # slot centre height
TSLOT_L = 126.8    # slot overall length
TSLOT_W = 5.1      # slot width

# hole diameters
D_S = 5.2          # small holes
D_M = 6.0          # medium holes
D_L = 6.5          # large holes (diagonal corners of the pattern)

# holes of one quadrant (x<0, z>0) -> mirrored into all four quadrants
QUAD_HOLES = [
    (-69.1, 145.4, D_M),
    (-12.25, 145.4, D_M),
    (-53.8, 130.3, D_M),
    (-12.3, 111.8, D_S),
    (-79.8, 107.1, D_S),
    (-43.1, 107.1, D_S),
    (-23.05, 104.1, D_M),
    (-12.3, 88.9, D_M),
    (-29.9, 86.5, D_M),
    (-23.05, 68.8, D_M),
    (-79.8, 61.2, D_S),
    (-43.1, 61.2, D_S),
    (-53.8, 53.8, D_L),
]
# holes on the vertical centre line (mirrored top/bottom)
CENTER_HOLES = [(0.0, 124.1, D_S), (0.0, 99.6, D_S)]
# bottom-only holes (mirrored left/right), opposite the top slot
BOTTOM_HOLES = [(-52.9, -138.0, D_S), (-24.4, -138.0, D_S)]


def cutter_wp():
    """Sketch plane behind the plate (y = +T); extruding 2*T along its
    normal (-Y) passes cleanly through the whole plate in one piece."""
    return cq.Workplane("XZ", origin=(0, T, 0))


# ---------------- plate body ----------------
plate = (
    cq.Workplane("XZ", origin=(0, T / 2.0, 0))   # front face at y=+T/2
    .rect(W, H)
    .extrude(T)                                  # to y=-T/2
    .edges("|Y")
    .fillet(R_CORNER)
)

# ---------------- hole pattern ----------------
holes = []
for (x, z, d) in QUAD_HOLES:
    for sx in (1, -1):
        for sz in (1, -1):
            holes.append((sx * x, sz * z, d))
for (x, z, d) in CENTER_HOLES:
    for sz in (1, -1):
        holes.append((x, sz * z, d))
for (x, z, d) in BOTTOM_HOLES:
    for sx in (1, -1):
        holes.append((sx * x, z, d))

by_d = {}
for (x, z, d) in holes:
    by_d.setdefault(d, []).append((x, z))

cutter = None
for d in sorted(by_d):
    c = cutter_wp().pushPoints(by_d[d]).circle(d / 2.0).extrude(2 * T)
    cutter = c if cutter is None else cutter.union(c)

# ---------------- slots ----------------
for sx in (1, -1):
    hand = (
        cutter_wp()
        .center(sx * HANDLE_X, 0)
        .slot2D(HANDLE_L, HANDLE_W, angle=90)
        .extrude(2 * T)
    )
    cutter = cutter.union(hand)

top_slot = (
    cutter_wp()
    .center(0, TSLOT_Z)
    .slot2D(TSLOT_L, TSLOT_W, angle=0)
    .extrude(2 * T)
)
cutter = cutter.union(top_slot)

result = plate.cut(cutter).clean()

VIEW = {"azimuth": 45, "elevation": 26}
